import cadquery as cq

# Driving dimensions (mm)
BASE_D = 50.0          # base disc diameter
BASE_H = 21.6          # base disc height
BASE_TOP_FILLET = 1.2  # rounded top rim of base
PIN_D = 10.1           # pin diameter
PIN_L = 50.3           # pin length above base top face
PIN_TOP_FILLET = 0.6   # rounded pin tip
SEAM_ANGLE = 45.0      # rotate about Z so cylinder seams sit out of the main view

# Base disc with rounded top rim, sharp bottom edge
base = cq.Workplane("XY").circle(BASE_D / 2.0).extrude(BASE_H)
base = base.faces(">Z").edges().fillet(BASE_TOP_FILLET)

# Pin (slightly sunk into the base for a clean union)
pin = (
    cq.Workplane("XY")
    .workplane(offset=BASE_H - 0.5)
    .circle(PIN_D / 2.0)
    .extrude(PIN_L + 0.5)
)
pin = pin.faces(">Z").edges().fillet(PIN_TOP_FILLET)

result = base.union(pin).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

VIEW = {"azimuth": 45, "elevation": 26}
